import cadquery as cq

# =====================================================================
#  Open-top enclosure / tray
#  - rounded rectangular box, open top
#  - shelf along the -X end with a through notch in the -X wall
#  - deeper pocket over the rest of the floor, with two triangular
#    corner blocks at the +X corners
#  - obround through-slot in the +X wall
#  - small rectangular window through the front (-Y) wall
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 90.0            # overall length along X
D = 70.0            # overall depth along Y
H = 28.0            # overall height along Z
T = 4.5             # wall thickness
R_OUT = 4.2         # outer vertical corner radius
R_BOT = 0.4         # small round on bottom outer edges

Z_SHELF = 14.6      # height of shelf / notch floor
Z_FLOOR = 4.6       # height of pocket floor
SHELF_W = 9.5       # shelf width (X) measured from inner face of -X wall
POCKET_INSET = 0.0  # optional ledge between upper cavity wall and pocket wall
POCKET_R = 2.25     # vertical round at the two -X corners of the pocket

NOTCH_W = 28.0      # width (Y) of notch in the -X wall (from top to shelf)
NOTCH_R = 0.5       # small round on the notch edges

GUSSET = 9.3        # leg length of triangular corner blocks (+X corners)

SLOT_L = 38.0       # slot length (Y) in +X wall
SLOT_H = 9.5        # slot height (Z)
SLOT_Z = 10.4       # slot centre height

RECT_X0 = -37.4     # small rectangular window in front wall (X range)
RECT_X1 = -26.5
RECT_Z0 = 19.8      # (Z range)
RECT_Z1 = 24.6

# ---------------- derived ----------------
xi0 = -W / 2 + T          # inner face of -X wall
xi1 = W / 2 - T           # inner face of +X wall
yi0 = -D / 2 + T          # inner face of front wall
yi1 = D / 2 - T           # inner face of back wall
px0 = xi0 + SHELF_W       # -X edge of pocket (shelf step)
px1 = xi1 - POCKET_INSET
py0 = yi0 + POCKET_INSET
py1 = yi1 - POCKET_INSET

# ---------------- outer body ----------------
body = (
    cq.Workplane("XY")
    .rect(W, D)
    .extrude(H)
    .edges("|Z")
    .fillet(R_OUT)
)
body = body.faces("<Z").edges().fillet(R_BOT)

# ---------------- upper cavity (down to the shelf) ----------------
cavity = (
    cq.Workplane("XY", origin=(0, 0, Z_SHELF))
    .center((xi0 + xi1) / 2, 0)
    .rect(xi1 - xi0, yi1 - yi0)
    .extrude(H)
)
body = body.cut(cavity)

# ---------------- pocket below the shelf ----------------
pocket = (
    cq.Workplane("XY", origin=(0, 0, Z_FLOOR))
    .center((px0 + px1) / 2, (py0 + py1) / 2)
    .rect(px1 - px0, py1 - py0)
    .extrude(Z_SHELF - Z_FLOOR + 0.5)
    .edges("|Z and <X")
    .fillet(POCKET_R)
)
body = body.cut(pocket)

# ---------------- triangular corner blocks (+X corners) ----------------
for sy in (1, -1):
    cy = py1 if sy > 0 else py0
    blk = (
        cq.Workplane("XY", origin=(0, 0, Z_FLOOR))
        .polyline([(px1, cy), (px1 - GUSSET, cy), (px1, cy - sy * GUSSET)])
        .close()
        .extrude(Z_SHELF - Z_FLOOR)
    )
    body = body.union(blk)

# ---------------- notch through the -X wall ----------------
notch = (
    cq.Workplane("XY", origin=(0, 0, Z_SHELF))
    .center(-W / 2 + T / 2, 0)
    .rect(T * 3, NOTCH_W)
    .extrude(H)
)
body = body.cut(notch)

# small rounds on the notch (stub-end vertical edges, stub top edges and
# concave bottom corners)
if NOTCH_R > 0:
    sel = cq.selectors.BoxSelector(
        (-W / 2 - 1, -NOTCH_W / 2 - 0.1, Z_SHELF - 0.1),
        (xi0 + 0.01, NOTCH_W / 2 + 0.1, H + 1),
    )
    body = body.edges(sel).fillet(NOTCH_R)

# ---------------- obround slot through the +X wall ----------------
slot = (
    cq.Workplane("YZ", origin=(W / 2 - T / 2, 0, SLOT_Z))
    .slot2D(SLOT_L, SLOT_H, 0)
    .extrude(T * 2, both=True)
)
body = body.cut(slot)

# ---------------- rectangular window through the front wall ----------------
win = (
    cq.Workplane("XZ", origin=(0, -D / 2 + T / 2, 0))
    .center((RECT_X0 + RECT_X1) / 2, (RECT_Z0 + RECT_Z1) / 2)
    .rect(RECT_X1 - RECT_X0, RECT_Z1 - RECT_Z0)
    .extrude(T * 2, both=True)
)
body = body.cut(win)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
